import math
import cadquery as cq

# ---------------------------------------------------------------
# Plain solid sphere (ball).
# Driving dimensions (mm)
# ---------------------------------------------------------------
SPHERE_DIAMETER = 50.0
RADIUS = SPHERE_DIAMETER / 2.0

# Orientation of the (geometrically irrelevant) B-rep seam of the sphere:
# pole axis horizontal along (-1,-1,0); seam meridian swung SEAM_DIP degrees
# below horizontal towards the back-left, where the reference views hide it.
SEAM_DIP_DEG = 55.0

VIEW = {"azimuth": 45, "elevation": 26}

_pole = cq.Vector(-1, -1, 0).normalized()
_a = math.radians(SEAM_DIP_DEG)
_back_left = cq.Vector(-1, 1, 0).normalized()
_seam = (_back_left * math.cos(_a) + cq.Vector(0, 0, -1) * math.sin(_a)).normalized()

_plane = cq.Plane(origin=(0, 0, 0), xDir=_seam, normal=_pole)

result = cq.Workplane(_plane).sphere(RADIUS)
